import math

import cadquery as cq
from OCP.BRepFilletAPI import BRepFilletAPI_MakeFillet

# ---------------- driving dimensions (mm) ----------------
LEN_X = 70.0        # overall length along X (back arm of the L)
LEN_Y = 78.7        # overall length along Y (left arm of the L)
ARM_W = 33.3        # width of both L arms
PLATE_T = 6.0       # plate thickness
BLOCK_H = 24.0      # total height of the two end blocks
BLOCK_L = 19.7      # length of each end block along its arm

R_BLOCK = 1.9       # fillet on block vertical and top edges
R_PLATE = 1.5       # fillet on the inner top edges of the plate
R_BOTTOM = 1.6      # fillet round the whole bottom outline

# plate hole near the outer corner of the L
CORNER_HOLE_OFF = 12.0   # distance of its centre from both outer edges
CORNER_HOLE_D = 9.2
CORNER_CSK_D = 15.0

# holes through the blocks (countersunk from below)
BLOCK_HOLE_D = 6.7
BLOCK_CSK_D = 12.4
CSK_ANGLE = 90.0

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- derived coordinates ----------------
x0, x1 = -LEN_X / 2.0, LEN_X / 2.0
y0, y1 = -LEN_Y / 2.0, LEN_Y / 2.0
xi = x0 + ARM_W          # x of the inner corner of the L
yi = y1 - ARM_W          # y of the inner corner of the L


def box(xa, xb, ya, yb, za, zb):
    return (
        cq.Workplane("XY")
        .box(xb - xa, yb - ya, zb - za, centered=False)
        .translate((xa, ya, za))
    )


# L shaped base plate
plate_pts = [(x0, y0), (xi, y0), (xi, yi), (x1, yi), (x1, y1), (x0, y1)]
plate = cq.Workplane("XY").polyline(plate_pts).close().extrude(PLATE_T)

# end blocks standing on the two arm ends, flush with the arm sides
block_a = box(x1 - BLOCK_L, x1, yi, y1, 0.0, BLOCK_H)   # +X end of the back arm
block_b = box(x0, xi, y0, y0 + BLOCK_L, 0.0, BLOCK_H)   # -Y end of the left arm

solid = plate.union(block_a).union(block_b).val()

# ---------------- edge treatment ----------------
EPS = 1e-3


def near(a, b):
    return abs(a - b) < EPS


def is_block_vertical(e):
    bb = e.BoundingBox()
    return (
        near(bb.xmin, bb.xmax)
        and near(bb.ymin, bb.ymax)
        and near(bb.zmax, BLOCK_H)
    )


def is_plate_inner_top(e):
    bb = e.BoundingBox()
    if not (near(bb.zmin, PLATE_T) and near(bb.zmax, PLATE_T)):
        return False
    return (near(bb.xmin, xi) and near(bb.xmax, xi)) or (
        near(bb.ymin, yi) and near(bb.ymax, yi)
    )


def is_at_z(z):
    def f(e):
        bb = e.BoundingBox()
        return near(bb.zmin, z) and near(bb.zmax, z)
    return f


def multi_fillet(shape, radius_edge_pairs):
    """One fillet operation with an individual radius per edge."""
    mk = BRepFilletAPI_MakeFillet(shape.wrapped)
    for r, e in radius_edge_pairs:
        mk.Add(r, e.wrapped)
    mk.Build()
    if mk.IsDone():
        out = cq.Shape.cast(mk.Shape())
        if out.isValid():
            return out
    # fallback: one radius per call, largest radius first
    for r in sorted({r for r, _ in radius_edge_pairs}, reverse=True):
        centres = [e.Center() for rr, e in radius_edge_pairs if rr == r]
        edges = [
            e for e in shape.Edges()
            if any((e.Center() - c).Length < 1e-3 for c in centres)
        ]
        if edges:
            shape = shape.fillet(r, edges)
    return shape


# vertical block edges together with the inner top edges of the plate
pairs = [(R_BLOCK, e) for e in solid.Edges() if is_block_vertical(e)]
pairs += [(R_PLATE, e) for e in solid.Edges() if is_plate_inner_top(e)]
solid = multi_fillet(solid, pairs)
# rounded tops of the blocks
solid = solid.fillet(R_BLOCK, [e for e in solid.Edges() if is_at_z(BLOCK_H)(e)])
# small round on the whole bottom outline
solid = solid.fillet(R_BOTTOM, [e for e in solid.Edges() if is_at_z(0.0)(e)])

# ---------------- countersunk holes (countersink on the underside) ----------------
corner_c = (x0 + CORNER_HOLE_OFF, y1 - CORNER_HOLE_OFF)
block_a_c = (x1 - BLOCK_L / 2.0, y1 - ARM_W / 2.0)
block_b_c = (x0 + ARM_W / 2.0, y0 + BLOCK_L / 2.0)


def csk_tool(cx, cy, d, dcsk, height):
    half = math.radians(CSK_ANGLE / 2.0)
    csk_depth = (dcsk - d) / 2.0 / math.tan(half)
    bore = cq.Solid.makeCylinder(d / 2.0, height + 2.0, cq.Vector(cx, cy, -1.0))
    cone = cq.Solid.makeCone(
        dcsk / 2.0 + 1.0 * math.tan(half), d / 2.0, csk_depth + 1.0,
        cq.Vector(cx, cy, -1.0),
    )
    return bore.fuse(cone)


for tool in (
    csk_tool(corner_c[0], corner_c[1], CORNER_HOLE_D, CORNER_CSK_D, PLATE_T),
    csk_tool(block_a_c[0], block_a_c[1], BLOCK_HOLE_D, BLOCK_CSK_D, BLOCK_H),
    csk_tool(block_b_c[0], block_b_c[1], BLOCK_HOLE_D, BLOCK_CSK_D, BLOCK_H),
):
    solid = solid.cut(tool)

result = cq.Workplane("XY").add(solid)
